import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0        # box length along X
D = 66.7         # box depth along Y
H = 20.0         # box height
T = 3.2          # wall thickness
F = 2.0          # floor thickness
GAP = 12.0       # gap between the two half-shells (hinge zone)

XC = -22.6       # X of the cradle / ring axis
ZC = H           # cradle axis lies on the parting plane

RIB_T = 3.4      # rib thickness
RIB_L = 28.7     # rib length along X
RIB_POS = (8.0, 33.35, 57.2)   # rib positions measured from hinge-side face

FR_RIB_TOP = 13.7   # front (lower) shell rib height
FR_NOTCH_R = 8.4    # concave notch radius in the front ribs
BK_RIB_TOP = 26.6   # back shell U-rib height
BK_U_HW = 7.3       # U-slot half width
BK_U_R = 8.4        # U-slot bottom radius (tube radius)

RING_RO = 14.1   # ring outer radius
RING_RI = 6.55   # ring bore radius
RING_OUT = 10.9  # ring protrusion beyond the back wall
RING_IN = 0.5    # ring boss standing proud of the inner wall face
RING_CB_R = 12.9  # counterbore radius at the open end of the ring
RING_CB_D = 10.9  # counterbore depth (down to the wall)

BIG_CUT_R = 14.3    # front wall cut (receives the ring when closed)
SMALL_CUT_R = 6.55  # hinge-side wall cut

DIV_T = 2.8      # divider thickness (back shell)

ARROW_Y0 = 40.0  # arrow tip, measured from the hinge-side face
ARROW_L = 10.0
ARROW_HL = 3.2   # head length
ARROW_HW = 1.9   # head half width
ARROW_T = 0.6    # head thickness
ARROW_SR = 1.3   # shaft radius

LATCH_X0, LATCH_X1 = 12.2, 36.3
LATCH_DEPTH = 7.6
LATCH_IN = 2.4
LATCH_WIN_X = (17.8, 31.2)   # catch window through the wall at the pocket
LATCH_WIN_Z = (8.5, 12.4)
LATCH_WIN_Y = 0.8            # window start, measured from the outer face

# hinge
HX0, HX1 = -13.5, 13.5
HN = 5
KN_R = 2.75
AX_Y = 2.8
PIN_R = 0.95
WEDGE_TOP = ZC - KN_R     # gusset top = underside of knuckles
WEDGE_W = 3.4             # gusset width at the top
WEDGE_BOT = 1.5

# small features in the back shell right compartment
TRAY_X0, TRAY_X1 = 5.6, 26.2
TRAY_LEN = 13.5
TRAY_TOP = 17.7
TRAY_H = 2.4
TRAY_WALL = 1.2
ROD_R = 1.0
CH_X = (30.7, 42.6)       # thin channel ribs
CH_LEN = 28.4
CH_T = 1.6
CH_H = 1.8
POST_R = 1.1
POST_HOLE_R = 0.55
WIRE_W, WIRE_H, WIRE_Z = 8.0, 3.0, 4.5

# tube (loose part)
TUBE_X = -76.8
TUBE_RO = 8.4
TUBE_RI = 6.75
TUBE_L = 59.0
PIN_RAD = 3.15
PIN_RI = 2.3
PIN_OUT = 10.5
PIN_YS = (13.3, -19.7)
GROOVE_YS = (23.3, -0.7, -26.0)
GROOVE_W = 3.3
GROOVE_Z = (4.0, 12.5)
GROOVE_DEPTH = 1.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_y(x, z, y0, y1, r, seam="bottom"):
    """cylinder along +Y; seam placed at the bottom (outer surfaces) or the
    top (bores) so it stays out of sight"""
    c = (cq.Workplane("XZ", origin=(0, y0, 0))
         .circle(r).extrude(-(y1 - y0)))
    ang = 90 if seam == "bottom" else -90
    c = c.rotate((0, 0, 0), (0, 1, 0), ang)
    return c.translate((x, 0, z))


def cyl_x(y, z, x0, x1, r, seam="bottom"):
    """cylinder along +X with the seam at the bottom or the top"""
    c = (cq.Workplane("YZ", origin=(x0, 0, 0))
         .circle(r).extrude(x1 - x0))
    ang = -90 if seam == "bottom" else 90
    c = c.rotate((0, 0, 0), (1, 0, 0), ang)
    return c.translate((0, y, z))


def cyl_z(x, y, z0, z1, r):
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .center(x, y).circle(r).extrude(z1 - z0))


def prism_x(pts, x0, x1):
    """extrude a YZ polygon along +X from x0 to x1"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close().extrude(x1 - x0))


def shell_box(y0, y1):
    outer = box(-W / 2, W / 2, y0, y1, 0, H)
    inner = box(-W / 2 + T, W / 2 - T, y0 + T, y1 - T, F, H + 1)
    return outer.cut(inner)


# ================= front (lower) shell =================
fy1 = -GAP / 2
fy0 = fy1 - D
front = shell_box(fy0, fy1)

for p in RIB_POS:
    yc = fy1 - p
    rib = box(XC - RIB_L / 2, XC + RIB_L / 2, yc - RIB_T / 2, yc + RIB_T / 2,
              F - 0.01, FR_RIB_TOP)
    rib = rib.cut(cyl_y(XC, ZC, yc - 5, yc + 5, FR_NOTCH_R))
    front = front.union(rib)

# big cut in far wall, small cut in hinge wall
front = front.cut(cyl_y(XC, ZC, fy0 - 1, fy0 + T + 1, BIG_CUT_R))
front = front.cut(cyl_y(XC, ZC, fy1 - T - 1, fy1 + 1, SMALL_CUT_R))
# latch pocket on the far wall + catch window through the wall below it
front = front.cut(box(LATCH_X0, LATCH_X1, fy0 - 1, fy0 + LATCH_IN,
                      H - LATCH_DEPTH, H + 1))
front = front.cut(box(LATCH_WIN_X[0], LATCH_WIN_X[1], fy0 + LATCH_WIN_Y,
                      fy0 + T + 0.5, LATCH_WIN_Z[0], LATCH_WIN_Z[1]))

# ================= back (upper) shell =================
by0 = GAP / 2
by1 = by0 + D
back = shell_box(by0, by1)
# divider
back = back.union(box(-DIV_T / 2, DIV_T / 2, by0 + 0.5, by1 - 0.5, F - 0.01, H))

for p in RIB_POS:
    yc = by0 + p
    rib = box(XC - RIB_L / 2, XC + RIB_L / 2, yc - RIB_T / 2, yc + RIB_T / 2,
              F - 0.01, BK_RIB_TOP)
    slab = box(XC - BK_U_HW, XC + BK_U_HW, yc - 5, yc + 5, ZC - BK_U_R - 1,
               BK_RIB_TOP + 5)
    ucut = cyl_y(XC, ZC, yc - 5, yc + 5, BK_U_R).union(
        box(XC - BK_U_HW, XC + BK_U_HW, yc - 5, yc + 5, ZC, BK_RIB_TOP + 5)
    ).intersect(slab)
    back = back.union(rib.cut(ucut))

# ring (cup) on the far wall
ring = cyl_y(XC, ZC, by1 - T - RING_IN, by1 + RING_OUT, RING_RO)
back = back.union(ring)
back = back.cut(cyl_y(XC, ZC, by1 - T - RING_IN - 1, by1 + RING_OUT + 1,
                      RING_RI, seam="top"))
back = back.cut(cyl_y(XC, ZC, by1 + RING_OUT - RING_CB_D, by1 + RING_OUT + 1,
                      RING_CB_R, seam="top"))
back = back.cut(cyl_y(XC, ZC, by0 - 1, by0 + T + 1, SMALL_CUT_R))
back = back.cut(box(LATCH_X0, LATCH_X1, by1 - LATCH_IN, by1 + 1,
                    H - LATCH_DEPTH, H + 1))

# direction arrow on the floor of the cradle compartment:
# rounded (half-round) shaft + flat triangular head, pointing at the hinge
ay0, ay1 = by0 + ARROW_Y0, by0 + ARROW_Y0 + ARROW_L
head = (cq.Workplane("XY", origin=(0, 0, F - 0.01))
        .polyline([(XC - ARROW_HW, ay0 + ARROW_HL), (XC + ARROW_HW, ay0 + ARROW_HL),
                   (XC, ay0)])
        .close().extrude(ARROW_T + 0.01))
shaft = cyl_y(XC, F, ay0 + ARROW_HL - 0.3, ay1, ARROW_SR)
shaft = shaft.faces(">Y").edges().fillet(0.9 * ARROW_SR)
shaft = shaft.intersect(box(XC - 2, XC + 2, ay0, ay1 + 1, F - 0.01, F + 2))
arrow = head.union(shaft)
back = back.union(arrow)

# hanging tray at the hinge wall (right compartment)
ty0 = by0 + T - 0.01
tray = box(TRAY_X0, TRAY_X1, ty0, ty0 + TRAY_LEN, TRAY_TOP - TRAY_H, TRAY_TOP)
tray = tray.edges("|Z and >Y").fillet(1.0)
# open frame (no floor)
tray = tray.cut(box(TRAY_X0 + TRAY_WALL, TRAY_X1 - TRAY_WALL, ty0 - 1,
                    ty0 + TRAY_LEN - TRAY_WALL, TRAY_TOP - TRAY_H - 1,
                    TRAY_TOP + 1))
# latch tongue: rod cantilevered from the frame's far side toward the wall
rod_x = TRAY_X1 - TRAY_WALL - ROD_R - 0.6
rod_z = TRAY_TOP - TRAY_H + ROD_R
rod_y0 = ty0 + 1.2
rod_y1 = ty0 + TRAY_LEN - TRAY_WALL + 0.01
rod = cyl_y(rod_x, rod_z, rod_y0 + ROD_R, rod_y1, ROD_R)
rod = rod.union(cq.Workplane("XY").sphere(ROD_R).translate((rod_x, rod_y0 + ROD_R, rod_z)))
tray = tray.union(rod)
back = back.union(tray)

# thin channel ribs + post, wire hole through the hinge wall
for cx in CH_X:
    chr_ = box(cx - CH_T / 2, cx + CH_T / 2, by0 + T - 0.01,
               by0 + T + CH_LEN - CH_T / 2, F - 0.01, F + CH_H)
    chr_ = chr_.union(cyl_z(cx, by0 + T + CH_LEN - CH_T / 2, F - 0.01,
                            F + CH_H, CH_T / 2))
    back = back.union(chr_)
chm = 0.5 * (CH_X[0] + CH_X[1])
post_y = by0 + T + CH_LEN
back = back.union(cyl_z(chm, post_y, F - 0.01, F + CH_H + 1.0, POST_R))
back = back.cut(cyl_z(chm, post_y, F + 0.5, F + CH_H + 2.0, POST_HOLE_R))
wire = (cq.Workplane("XZ", origin=(0, by0 - 1, 0)).center(chm, WIRE_Z)
        .slot2D(WIRE_W, WIRE_H).extrude(-(T + 2)))
back = back.cut(wire)

# ================= hinge =================
seg = (HX1 - HX0) / HN
hinge = None
for i in range(HN):
    x0 = HX0 + i * seg + (0.2 if i > 0 else 0)
    x1 = HX0 + (i + 1) * seg - (0.2 if i < HN - 1 else 0)
    if i % 2 == 0:   # knuckle of back shell
        k = cyl_x(AX_Y, ZC, x0, x1, KN_R).union(
            box(x0, x1, AX_Y, by0 + 0.01, ZC - KN_R, ZC + KN_R))
    else:            # knuckle of front shell
        k = cyl_x(-AX_Y, ZC, x0, x1, KN_R).union(
            box(x0, x1, fy1 - 0.01, -AX_Y, ZC - KN_R, ZC + KN_R))
    hinge = k if hinge is None else hinge.union(k)
hinge = hinge.cut(cyl_x(AX_Y, ZC, HX0 - 1, HX1 + 1, PIN_R, seam="top"))
hinge = hinge.cut(cyl_x(-AX_Y, ZC, HX0 - 1, HX1 + 1, PIN_R, seam="top"))

# triangular gussets under the knuckle rows
wedge_b = prism_x([(by0 + 0.01, WEDGE_BOT), (by0 + 0.01, WEDGE_TOP),
                   (by0 - WEDGE_W, WEDGE_TOP)], HX0, HX1)
wedge_f = prism_x([(fy1 - 0.01, WEDGE_BOT), (fy1 + WEDGE_W, WEDGE_TOP),
                   (fy1 - 0.01, WEDGE_TOP)], HX0, HX1)

back = back.union(wedge_b)
front = front.union(wedge_f)
cases = front.union(back).union(hinge)

# ================= loose tube with hollow cross pins =================
tube = cyl_y(TUBE_X, TUBE_RO, -TUBE_L / 2, TUBE_L / 2, TUBE_RO)
for py in PIN_YS:
    tube = tube.union(cyl_x(py, TUBE_RO, TUBE_X - TUBE_RO - PIN_OUT,
                            TUBE_X + TUBE_RO + PIN_OUT, PIN_RAD))
groove_ring = cyl_y(TUBE_X, TUBE_RO, -TUBE_L, TUBE_L, TUBE_RO + 1).cut(
    cyl_y(TUBE_X, TUBE_RO, -TUBE_L, TUBE_L, TUBE_RO - GROOVE_DEPTH))
for gy in GROOVE_YS:
    zb = GROOVE_Z[0] + GROOVE_W / 2
    cutter = box(TUBE_X - TUBE_RO - 1, TUBE_X + TUBE_RO + 1,
                 gy - GROOVE_W / 2, gy + GROOVE_W / 2, zb, GROOVE_Z[1])
    cutter = cutter.union(cyl_x(gy, zb, TUBE_X - TUBE_RO - 1,
                                TUBE_X + TUBE_RO + 1, GROOVE_W / 2))
    tube = tube.cut(cutter.intersect(groove_ring))
tube = tube.cut(cyl_y(TUBE_X, TUBE_RO, -TUBE_L / 2 - 1, TUBE_L / 2 + 1, TUBE_RI,
                      seam="top"))
for py in PIN_YS:
    tube = tube.cut(cyl_x(py, TUBE_RO, TUBE_X - TUBE_RO - PIN_OUT - 1,
                          TUBE_X + TUBE_RO + PIN_OUT + 1, PIN_RI, seam="top"))

result = cases.union(tube)

VIEW = {"azimuth": 45, "elevation": 26}
